import math
import cadquery as cq
from OCP.gp import gp_Ax2, gp_Pnt, gp_Dir
from OCP.BRepPrimAPI import BRepPrimAPI_MakeCylinder

# ---------------- driving dimensions (mm) ----------------
N = 16                 # number of tubes / lobes
THETA0 = 11.25         # angular offset of first lobe (deg)
R_F = 50.85            # tube axis radius where it pierces the front face
R_B = 42.4             # tube axis radius where it pierces the back face
TWIST = 11.25          # clockwise (seen from front) twist of tubes front->back (deg)
R_T = 9.0              # tube outer radius (right circular cylinder)
R_H = 6.1              # tube bore radius
L = 28.9               # overall depth (along +Y)
T_PLATE = 3.0          # front plate thickness (bores stop here)
R_PLATE = 50.3         # central plate radius
SLV_DEPTH = 4.0        # depth of the curved slots (cut along the tube lean)

# sliver (curved slot) outline, in polar coords relative to its lobe:
# (delta_angle_deg, radius_mm).  Inner (counter-clockwise) edge, outer->tip
SLV_E1 = [(12.10, 51.74), (10.65, 47.88), (8.25, 44.10), (4.97, 40.43),
          (-0.12, 37.08), (-5.6, 35.16), (-14.87, 34.86)]
# edge hugging the lobe, tip->corner
SLV_E2 = [(-14.87, 34.86), (-6.63, 38.2), (-1.94, 41.28), (0.93, 43.98)]
# edge cutting into the lobe rim, corner->outer
SLV_E3 = [(0.93, 43.98), (2.2, 44.01), (4.53, 44.34), (6.63, 45.34),
          (8.42, 46.79), (9.66, 48.67), (10.45, 51.0)]
SLV_CLOSE = [(10.7, 53.5), (12.3, 53.5)]

VIEW = {"azimuth": 45, "elevation": 26}


def polar(rho, ang_deg):
    a = math.radians(ang_deg)
    return rho * math.cos(a), rho * math.sin(a)


def pt(base_deg, d_r, y=0.0):
    x, z = polar(d_r[1], base_deg + d_r[0])
    return cq.Vector(x, y, z)


def cylinder(r, base, axis, length, seam):
    """Right circular cylinder with its seam line placed toward `seam`."""
    n = axis.normalized()
    sx = seam - n * seam.dot(n)
    ax = gp_Ax2(gp_Pnt(base.x, base.y, base.z), gp_Dir(n.x, n.y, n.z),
                gp_Dir(sx.x, sx.y, sx.z))
    return cq.Solid(BRepPrimAPI_MakeCylinder(ax, r, length).Shape())


def slab(y0, y1):
    return cq.Solid.makeBox(300, y1 - y0, 300, cq.Vector(-150, y0, -150))


def sliver(base_deg, y0, vec):
    e1 = cq.Edge.makeSpline([pt(base_deg, p, y0) for p in SLV_E1])
    e2 = cq.Edge.makeSpline([pt(base_deg, p, y0) for p in SLV_E2])
    e3 = cq.Edge.makeSpline([pt(base_deg, p, y0) for p in SLV_E3])
    pc = [pt(base_deg, SLV_E3[-1], y0)] + [pt(base_deg, p, y0) for p in SLV_CLOSE] \
        + [pt(base_deg, SLV_E1[0], y0)]
    lines = [cq.Edge.makeLine(pc[i], pc[i + 1]) for i in range(len(pc) - 1)]
    w = cq.Wire.assembleEdges([e1, e2, e3] + lines)
    f = cq.Face.makeFromWires(w)
    return cq.Solid.extrudeLinear(f, vec)


# front plate (straight disk)
solid = cq.Solid.makeCylinder(R_PLATE, T_PLATE, cq.Vector(0, 0, 0), cq.Vector(0, 1, 0))

EXT = 12.0
tubes, bores, slivers = [], [], []
for k in range(N):
    th = THETA0 + 360.0 / N * k
    fx, fz = polar(R_F, th)
    bx, bz = polar(R_B, th - TWIST)
    F = cq.Vector(fx, 0, fz)
    d = cq.Vector(bx - fx, L, bz - fz)
    n = d.normalized()
    cw = cq.Vector(math.sin(math.radians(th)), 0, -math.cos(math.radians(th)))
    radial = cq.Vector(math.cos(math.radians(th)), 0, math.sin(math.radians(th)))
    tubes.append(cylinder(R_T, F - n * EXT, n, d.Length + 2 * EXT, cw))
    bores.append(cylinder(R_H, F - n * EXT, n, d.Length + 2 * EXT, radial))
    sd = (SLV_DEPTH + 0.5) / L
    sv = sliver(th, -0.5, cq.Vector(d.x * sd, L * sd, d.z * sd))
    slivers.append(sv.translate(cq.Vector(-d.x * 0.5 / L, 0, -d.z * 0.5 / L)))

for t in tubes:
    solid = solid.fuse(t)
solid = solid.intersect(slab(0.0, L))
bore_all = bores[0]
for b in bores[1:]:
    bore_all = bore_all.fuse(b)
solid = solid.cut(bore_all.intersect(slab(T_PLATE, L + 5.0)))
for s_ in slivers:
    solid = solid.cut(s_)
solid = solid.clean()

result = cq.Workplane("XY").add(solid)
